import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
FAN = 40.0            # fan plate size (40 mm fan)
FAN_PITCH = 32.0      # fan screw pitch
FAN_HOLE_D = 3.3
FAN_HOLE_DEPTH = 10.0
FAN_OPEN_D = 35.5
PLATE_T = 3.0
TILT = 31.8           # fan plate tilt from vertical (deg)
HW = 20.0             # duct half width (x)
WALL = 2.5            # duct wall
RIB_T = 1.1           # divider ribs
FUN_A, FUN_B, FUN_ZC = 14.0, 11.0, 13.0   # funnel end (ellipse on the back wall)
FIN_DROP = 44.0       # horizontal divider slope (deg below horizontal, going back)
TOP_Y, TOP_Z = -6.4, 41.7   # outer top edge of the fan plate (y, z)
Y_BACK = -1.2         # back face of the duct
TOP_FILLET = 3.0      # rounded top/back edge of the duct
OUTLET_X = (-11.0, 11.0)
OUTLET_ZTOP = 11.9
BEV_X1 = 10.0

TUBE_X, TUBE_Y = 18.5, 0.0
TUBE_R = 6.5
TUBE_RI = 5.0
TUBE_H = 65.8
RING1 = (58.3, 59.8)   # lower groove-mount collar (z range)
RING2 = (62.6, 64.1)   # upper collar
GROOVE_R = 6.05
RING_R = 7.15
LIP_R = 5.85
CUT_X = 20.0          # tube is cut open beyond this plane

BR_Y0, BR_Y1 = 12.5, 17.0     # bracket plate thickness range (y)
BR_X0 = -43.2                 # bracket left edge
EAR_X, EAR_Z, EAR_R = -18.8, 31.6, 7.8
HOLE_D = 8.0
EAR_HOLE_D = 8.0
EAR_HOLE_X = -18.5
LOW_HOLE = (-35.7, 12.7)
SLOPE = 46.6                  # slanted edge of bracket (deg)
EDGE_CH = 1.0

CONN_X1 = -11.0               # connection block  x -HW .. CONN_X1
CONN_H = 22.0
CONN_SLOT_Y = 7.5
CONN_HOLES = (5.0, 8.8, 12.6)

s, c = math.sin(math.radians(TILT)), math.cos(math.radians(TILT))

# --------------------------------------------------------------- duct body
T_out = (TOP_Y, TOP_Z)
B_out = (TOP_Y - FAN * s, TOP_Z - FAN * c)

# bottom arc: circle through B_out, ARC_MID and ARC_LOW (y, z)
ARC_MID = (-15.25, 2.4)
ARC_LOW = (-6.4, 0.6)


def circle_3pt(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    a11, a12 = 2 * (x2 - x1), 2 * (y2 - y1)
    a21, a22 = 2 * (x3 - x1), 2 * (y3 - y1)
    b1 = x2 ** 2 - x1 ** 2 + y2 ** 2 - y1 ** 2
    b2 = x3 ** 2 - x1 ** 2 + y3 ** 2 - y1 ** 2
    det = a11 * a22 - a12 * a21
    cx = (b1 * a22 - a12 * b2) / det
    cy = (a11 * b2 - b1 * a21) / det
    return cx, cy, math.hypot(x1 - cx, y1 - cy)


ARC_CY, ARC_CZ, ARC_R = circle_3pt(B_out, ARC_MID, ARC_LOW)
z_end = ARC_CZ - math.sqrt(ARC_R ** 2 - (Y_BACK - ARC_CY) ** 2)


def duct_profile(wp):
    return (wp.moveTo(*T_out)
            .lineTo(*B_out)
            .threePointArc(ARC_MID, (Y_BACK, z_end))
            .lineTo(Y_BACK, TOP_Z - TOP_FILLET)
            .threePointArc((Y_BACK - TOP_FILLET * (1 - math.sqrt(0.5)),
                            TOP_Z - TOP_FILLET * (1 - math.sqrt(0.5))),
                           (Y_BACK - TOP_FILLET, TOP_Z))
            .close())


duct_outer = duct_profile(cq.Workplane("YZ", origin=(-HW, 0, 0))).extrude(2 * HW)

# cavity limits: side walls, curved floor and back wall (the funnel defines the rest)
cav_box = (cq.Workplane("XY").box(2 * (HW - WALL), 80, 80, centered=(True, False, False))
           .translate((0, Y_BACK - WALL - 80, -10)))
cav_floor = (cq.Workplane("YZ", origin=(-HW, 0, 0)).center(ARC_CY, ARC_CZ)
             .circle(ARC_R - WALL).extrude(2 * HW))
cavity = cav_box.intersect(cav_floor)

# fan plate frame
FC = (0.0, TOP_Y - 20 * s, TOP_Z - 20 * c)          # centre of outer fan face
n_out = (0.0, -c, s)
fan_pl = cq.Plane(origin=FC, xDir=(1, 0, 0), normal=n_out)

# divider ribs (kept inside the cavity)
rib_v = cq.Workplane("XY").box(RIB_T, 200, 200)
fd = math.radians(FIN_DROP)
fin_pl = cq.Plane(origin=FC, xDir=(1, 0, 0), normal=(0, math.sin(fd), math.cos(fd)))
rib_h = cq.Workplane(fin_pl).rect(2 * HW, 90).extrude(RIB_T / 2, both=True)
tube_keep = cq.Workplane("XY").center(TUBE_X, TUBE_Y).circle(TUBE_R).extrude(80)
# the air path is a slightly converging funnel behind the fan opening
w_fan = cq.Wire.makeEllipse(FAN_OPEN_D / 2, FAN_OPEN_D / 2,
                            cq.Vector(*FC) + cq.Vector(*n_out) * 0.5, cq.Vector(*n_out),
                            cq.Vector(1, 0, 0))
w_back = cq.Wire.makeEllipse(FUN_A, FUN_B, cq.Vector(0, Y_BACK - WALL - 0.2, FUN_ZC),
                             cq.Vector(0, -1, 0), cq.Vector(1, 0, 0))
funnel = cq.Workplane("XY").add(cq.Solid.makeLoft([w_fan, w_back]))
cavity = cavity.intersect(funnel)
cavity = cavity.cut(rib_v).cut(rib_h).cut(tube_keep)

duct = duct_outer.cut(cavity)

# fan screw holes (deep, through the duct corners); the opening itself is the
# mouth of the funnel
for hu, hv in ((-1, -1), (-1, 1), (1, -1), (1, 1)):
    # the hole next to the tube is kept short so it does not break into the bore
    depth = 4.5 if (hu, hv) == (1, 1) else FAN_HOLE_DEPTH
    duct = duct.cut(cq.Workplane(fan_pl).workplane(offset=0.5)
                    .center(hu * FAN_PITCH / 2, hv * FAN_PITCH / 2)
                    .circle(FAN_HOLE_D / 2).extrude(-(depth + 0.5)))

# lower outlet through the back wall (below the horizontal divider)
duct = duct.cut(cq.Workplane("XY").box(OUTLET_X[1] - OUTLET_X[0], 6.0, OUTLET_ZTOP - 1.0,
                                       centered=False)
                .translate((OUTLET_X[0], Y_BACK - 4.0, 1.0)))
# bevel along the lower back edge of the duct (clears the lower mounting slot)
BEV_Z, BEV_Y = 7.0, 5.3
bev_k = BEV_Z / BEV_Y
duct = duct.cut(cq.Workplane("YZ", origin=(-HW - 1, 0, 0))
                .polyline([(Y_BACK - BEV_Y - 1.0 / bev_k, -1.0), (Y_BACK + 1.7, -1.0),
                           (Y_BACK + 1.7, BEV_Z + 1.7 * bev_k)]).close()
                .extrude(HW + 1 + BEV_X1))

# ------------------------------------------------------------------ tube
BELL_R = 7.9           # outer radius of the bell mouth at the bottom
BELL_RI = 7.3          # inner radius of the bell mouth at the bottom
BELL_H = 4.0           # height of the flare (tangent to the tube above)


def tangent_arc_mid(r_top, r_bot, h):
    """Mid point of the arc that is vertical-tangent at (r_top, h) and passes (r_bot, 0)."""
    d = r_bot - r_top
    rf = (d * d + h * h) / (2 * d)
    cx, cz = r_top + rf, h
    a0 = math.atan2(0 - cz, r_bot - cx)
    a1 = math.pi
    am = (a0 + a1) / 2 if a0 > 0 else (a0 + 2 * math.pi + a1) / 2
    return (cx + rf * math.cos(am), cz + rf * math.sin(am))


tube = (cq.Workplane("XZ", origin=(TUBE_X, TUBE_Y, 0))
        .moveTo(0, 0).lineTo(BELL_R, 0)
        .threePointArc(tangent_arc_mid(TUBE_R, BELL_R, BELL_H), (TUBE_R, BELL_H))
        .lineTo(TUBE_R, RING1[0])
        .threePointArc((RING_R, sum(RING1) / 2), (GROOVE_R, RING1[1]))
        .lineTo(GROOVE_R, RING2[0])
        .threePointArc((RING_R, sum(RING2) / 2), (LIP_R, RING2[1]))
        .lineTo(LIP_R, TUBE_H - 0.4).lineTo(LIP_R - 0.4, TUBE_H)
        .lineTo(0, TUBE_H).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
bore = (cq.Workplane("XZ", origin=(TUBE_X, TUBE_Y, 0))
        .moveTo(0, -1).lineTo(BELL_RI, -1).lineTo(BELL_RI, 0)
        .threePointArc(tangent_arc_mid(TUBE_RI, BELL_RI, BELL_H), (TUBE_RI, BELL_H))
        .lineTo(TUBE_RI, TUBE_H + 1).lineTo(0, TUBE_H + 1).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))

# small cross-hole from the duct into the tube
ang = math.atan2(-0.78, -0.625)
air_hole = (cq.Workplane(cq.Plane(origin=(TUBE_X, TUBE_Y, 36.0), xDir=(0, 0, 1),
                                  normal=(math.cos(ang), math.sin(ang), 0)))
            .circle(1.5).extrude(9.0))

# ------------------------------------------------------------ bracket plate
a = math.radians(SLOPE)
nl = (-math.sin(a), math.cos(a))
tp = (EAR_X + EAR_R * nl[0], EAR_Z + EAR_R * nl[1])
z_left = tp[1] - math.tan(a) * (tp[0] - BR_X0)
x_right = EAR_X + EAR_R
mid_ear = (EAR_X + EAR_R * math.cos(math.radians(60)), EAR_Z + EAR_R * math.sin(math.radians(60)))
bracket = (cq.Workplane("XZ", origin=(0, BR_Y0, 0))
           .moveTo(BR_X0, 0).lineTo(x_right, 0).lineTo(x_right, EAR_Z)
           .threePointArc(mid_ear, tp).lineTo(BR_X0, z_left).close()
           .extrude(-(BR_Y1 - BR_Y0)))
# small chamfer along the front edge of the slanted side and the ear
_sel = []
for e in bracket.faces("<Y").edges().vals():
    if e.geomType() == "CIRCLE" and abs(e.radius() - EAR_R) < 0.01:
        _sel.append(e)
    elif e.geomType() == "LINE":
        d = e.endPoint() - e.startPoint()
        if abs(d.x) > 1 and abs(d.z) > 1:
            _sel.append(e)
bracket = bracket.newObject(_sel).chamfer(EDGE_CH)
bracket = bracket.edges("|Y").edges("<X").fillet(2.5)
for (hx, hz), hd in ((LOW_HOLE, HOLE_D), ((EAR_HOLE_X, EAR_Z), EAR_HOLE_D)):
    bracket = bracket.cut(cq.Workplane("XZ", origin=(0, 30, 0)).center(hx, hz)
                          .circle(hd / 2).extrude(40))

# shallow relief pocket on the front face next to the duct
POCK_X0, POCK_Z0, POCK_D = -31.5, 7.7, 1.2
bracket = bracket.cut(cq.Workplane("XZ", origin=(0, BR_Y0 + POCK_D, 0))
                      .polyline([(POCK_X0, -1), (-HW + 0.5, -1),
                                 (-HW + 0.5, POCK_Z0 + (POCK_X0 + HW - 0.5) * -1.07),
                                 (POCK_X0, POCK_Z0)]).close()
                      .extrude(5))

# connection block between duct and bracket (chamfered on the outer top edge)
conn = (cq.Workplane("XY").box(CONN_X1 + HW, BR_Y0 - Y_BACK + 1.0, CONN_H, centered=False)
        .translate((-HW, Y_BACK - 0.5, 0)))
conn = conn.edges("|Y and >Z").edges("<X").chamfer(3.0)
# small gusset between the connection block and the duct back
conn = conn.union(cq.Workplane("XY")
                  .polyline([(CONN_X1 - 0.5, Y_BACK), (CONN_X1 + 2.3, Y_BACK),
                             (CONN_X1 - 0.5, Y_BACK + 3.6 + 0.65)]).close()
                  .extrude(CONN_H))

# ---------------------------------------------------------------- rail block
RAIL_X0 = 11.5
RAIL_Y0, RAIL_Y1, RAIL_Y2 = 5.0, 16.8, 22.5     # body / dovetail-like mounting tongue
RAIL_H, TONGUE_Z0 = 24.5, 2.4
NOTCH_Y0, NOTCH_Y1, NOTCH_X1 = 16.8, 19.4, 15.3
rail = (cq.Workplane("XY").box(CUT_X - RAIL_X0, RAIL_Y1 - RAIL_Y0, RAIL_H, centered=False)
        .translate((RAIL_X0, RAIL_Y0, 0)))
tongue = (cq.Workplane("XY").box(CUT_X - 12.0, RAIL_Y2 - RAIL_Y1, RAIL_H - TONGUE_Z0,
                                 centered=False).translate((12.0, RAIL_Y1, TONGUE_Z0)))
# round-ended notch that forms the neck of the tongue
nw = NOTCH_Y1 - NOTCH_Y0
tongue = tongue.cut(cq.Workplane("XY", origin=(0, 0, 0))
                    .center((8.0 + NOTCH_X1) / 2, (NOTCH_Y0 + NOTCH_Y1) / 2)
                    .slot2D(NOTCH_X1 - 8.0, nw).extrude(40))
# shallow pocket on the back face of the tongue
tongue = tongue.cut(cq.Workplane("XY").box(6.0, 2.0, RAIL_H - TONGUE_Z0 - 6.0, centered=False)
                    .translate((12.0 - 0.01, RAIL_Y2 - 1.0, TONGUE_Z0 + 3.0)))
rail = rail.union(tongue)

# gusset between tube and duct back
GUS_H = 8.0
GUS_TOP = TOP_Z - TOP_FILLET
gusset = (cq.Workplane("XY", origin=(0, 0, GUS_TOP - GUS_H))
          .polyline([(9.0, Y_BACK), (13.0, Y_BACK), (13.0, 4.0)]).close()
          .extrude(GUS_H))
# taper the underside of the gusset (tall at the duct, vanishing towards the back)
g_zb, g_zt = GUS_TOP - GUS_H, GUS_TOP
g_k = (g_zt - g_zb) / (4.0 - Y_BACK)
gusset = gusset.cut(cq.Workplane("YZ", origin=(0, 0, 0))
                    .polyline([(Y_BACK - 1, g_zb - 1), (5.0, g_zb - 1),
                               (5.0, g_zb + g_k * (5.0 - Y_BACK)),
                               (Y_BACK - 1, g_zb - g_k)]).close()
                    .extrude(30, both=True))

# ---------------------------------------------------------------- assemble
body = duct.union(tube).union(bracket).union(conn).union(rail).union(gusset)
body = body.cut(bore).cut(air_hole)

# open the tube on the +X side
body = body.cut(cq.Workplane("XY").box(20, 60, 200, centered=(False, True, False))
                .translate((CUT_X, 0, -10)))

# screw-access channel in front of the upper bracket hole
body = body.cut(cq.Workplane("XZ", origin=(0, BR_Y0, 0)).center(EAR_X - 1.0, EAR_Z)
                .circle(2.8).extrude(40))

# 3-hole slots on both sides of the duct and on the connection block
def slot_cutter(x_face, y_c, z0, z1, width, depth, r_top):
    """Recessed vertical channel (open at the bottom) on an X-facing face."""
    b = (cq.Workplane("XY").box(2 * depth, width, z1 - z0, centered=(True, True, False))
         .translate((x_face, y_c, z0)))
    return b.edges("|X and >Z").fillet(r_top)


SLOT_W, SLOT_D = 5.9, 2.2
HOLES3 = (6.5, 10.4, 14.4)
for sx in (-1, 1):
    xf = sx * HW
    body = body.cut(slot_cutter(xf, -13.65, -1.0, 17.9, SLOT_W, SLOT_D, 1.2))
    for zh in HOLES3:
        body = body.cut(cq.Workplane("YZ", origin=(xf - 5 * sx, 0, 0)).center(-13.65, zh)
                        .circle(1.25).extrude(12 if sx > 0 else -12))

body = body.cut(slot_cutter(CONN_X1, CONN_SLOT_Y, -1.0, 17.9, SLOT_W, SLOT_D, 1.2))
for zh in CONN_HOLES:
    body = body.cut(cq.Workplane("YZ", origin=(CONN_X1 - 7, 0, 0)).center(CONN_SLOT_Y, zh)
                    .circle(1.25).extrude(8))

# 4-hole recesses on the rail block (deep on +X, shallow on -X), countersunk through holes
REC_Y0, REC_Y1, REC_Z1 = 5.5, 12.9, 19.6
REC_D_OUT, REC_D_IN = 3.0, 1.0
HOLES4 = (3.6, 7.8, 11.9, 15.8)
HOLE4_Y = 9.2
body = body.cut(slot_cutter(CUT_X, (REC_Y0 + REC_Y1) / 2, -1.0, REC_Z1,
                            REC_Y1 - REC_Y0, REC_D_OUT, 1.5))
body = body.cut(slot_cutter(RAIL_X0, (REC_Y0 + REC_Y1) / 2, -1.0, REC_Z1,
                            REC_Y1 - REC_Y0, REC_D_IN, 1.5))
for zh in HOLES4:
    body = body.cut(cq.Workplane("YZ", origin=(RAIL_X0 - 2, 0, 0)).center(HOLE4_Y, zh)
                    .circle(0.9).extrude(CUT_X - RAIL_X0 + 4))
    body = body.cut(cq.Workplane("YZ", origin=(CUT_X - REC_D_OUT + 0.01, 0, 0))
                    .center(HOLE4_Y, zh).circle(1.6).extrude(-0.8))

result = body
